import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R_OUT = 50.0          # outer radius of base disk and wall
T_OUTER = 2.3         # outer layer thickness of the wall
T_INNER = 2.3         # inner layer (lap) thickness of the wall
R_MID = R_OUT - T_OUTER
R_IN = R_MID - T_INNER

BASE_T = 8.0          # base disk thickness
POCKET_D = 3.0        # depth of recessed floor inside the rim
POCKET_R = R_MID      # floor pocket radius (leaves a rim of T_OUTER)

H_OUTER = 158.7       # top of the outer wall layer
LIP_H = 2.9           # inner lap lip standing above the outer layer
Z_STEP = 83.1         # height where the inner layer end changes
END_RECESS = 4.1      # upper inner layer ends set back behind the x=0 plane
END_PROTRUDE = 4.4    # lower inner layer ends stick out past the x=0 plane

HOLE_D = 5.3          # base holes
BOLT_R = 39.4         # bolt circle radius
HOLE_ANGLES = (30.0, 150.0, 270.0)

# lettering "S.P.I" cut through the wall, centred on the -X side,
# reading upward (+Z) from outside, letter tops toward +Y (bold serif style)
CAP_H = 30.3          # cap height of the letters (measured along Y)
BASELINE_Y = -15.0    # baseline position (along Y)
S_Z0, S_W = 36.1, 20.7    # "S": start height and width along Z
P_Z0, P_W = 72.3, 24.85   # "P"
I_Z0, I_W = 111.3, 15.3   # "I"
STEM = 6.8            # main stem weight of I and P
SERIF_T = 2.5         # serif thickness
BRACKET_R = 1.5       # serif bracket radius
P_STEM_AT = 0.16      # P: stem offset from the letter start (fraction of width)
P_FOOT = 0.61         # P: foot serif length (fraction of width)
P_BOWL_AT = 0.39      # P: bowl bottom (fraction of cap height)
P_COUNTER = 0.71      # P: far side of the counter (fraction of width)
S_LEFT = 0.8          # S: gap left of the upper bowl
S_STROKE = 3.4        # S: hairline stroke width (before stretching)
S_STRETCH = 1.2       # S: horizontal stretch (gives thicker upright curves)
S_R_UP = 5.5          # S: centre-line radius of the upper bowl
S_R_LOW = 6.2         # S: centre-line radius of the lower bowl
S_END_TOP = 0.0       # S: end angles of the stroke (deg)
S_END_BOT = 180.0
S_BALL_D = 6.5        # S: ball terminal diameter
DOT_D = 6.4           # full stops
DOT_Z = (65.2, 104.0)

BIG = 500.0

# ---------------- base disk with recessed floor ----------------
# (rotated so the cylinder seam lies on the wall end at -Y)
base = cq.Workplane("XY").circle(R_OUT).extrude(BASE_T).rotate((0, 0, 0), (0, 0, 1), -90)
pocket = (
    cq.Workplane("XY")
    .workplane(offset=BASE_T - POCKET_D)
    .circle(POCKET_R)
    .extrude(POCKET_D + 1.0)
)
base = base.cut(pocket)


def half_space_x(xmax, z0, z1):
    """box covering x <= xmax between heights z0 and z1"""
    return (
        cq.Workplane("XY")
        .box(BIG, BIG, z1 - z0, centered=(False, True, False))
        .translate((xmax - BIG, 0, z0))
    )


def ring(r0, r1, z0, z1):
    return (
        cq.Workplane("XY")
        .workplane(offset=z0)
        .circle(r1)
        .circle(r0)
        .extrude(z1 - z0)
    )


# outer layer: exact half cylinder on the -X side
outer = ring(R_MID, R_OUT, 0.0, H_OUTER).intersect(half_space_x(0.0, -1.0, H_OUTER + 1.0))

# inner layer, lower part: ends protrude past x=0
z_floor = BASE_T - POCKET_D
inner_low = ring(R_IN, R_MID, z_floor, Z_STEP).intersect(
    half_space_x(END_PROTRUDE, z_floor - 1.0, Z_STEP + 1.0)
)
# inner layer, upper part with lip: ends recessed behind x=0
inner_up = ring(R_IN, R_MID, Z_STEP, H_OUTER + LIP_H).intersect(
    half_space_x(-END_RECESS, Z_STEP - 1.0, H_OUTER + LIP_H + 1.0)
)

body = base.union(outer).union(inner_low).union(inner_up)

# ---------------- holes in the base ----------------
pts = [(0.0, 0.0)] + [
    (BOLT_R * math.cos(math.radians(a)), BOLT_R * math.sin(math.radians(a)))
    for a in HOLE_ANGLES
]
holes = (
    cq.Workplane("XY")
    .workplane(offset=-1.0)
    .pushPoints(pts)
    .circle(HOLE_D / 2.0)
    .extrude(BASE_T + 2.0)
)
body = body.cut(holes)

# ---------------- lettering cut through the wall ----------------
X_CUT_IN = -(R_IN - 4.0)          # cutters start inside the wall ...
CUT_DEPTH = (R_OUT - R_IN) + 8.0  # ... and run out through the outside


def arc3(c, r, a0, a1):
    """start, middle and end point of a circular arc (angles in degrees)"""
    p = lambda a: (c[0] + r * math.cos(math.radians(a)),
                   c[1] + r * math.sin(math.radians(a)))
    return p(a0), p(0.5 * (a0 + a1)), p(a1)


def closed_wire(start, segs):
    """segs: ("L", pt) straight line or ("A", centre, radius, a0, a1) arc"""
    wp = cq.Workplane("XY").moveTo(*start)
    for sg in segs:
        if sg[0] == "L":
            wp = wp.lineTo(*sg[1])
        else:
            _, mid, end = arc3(sg[1], sg[2], sg[3], sg[4])
            wp = wp.threePointArc(mid, end)
    return wp.close().wire().val()


# glyphs are drawn in a local (u, v) frame: u along the reading direction,
# v up the letter from the baseline
def glyph_I(W):
    H, t, rb = CAP_H, SERIF_T, BRACKET_R
    a, b = (W - STEM) / 2.0, (W + STEM) / 2.0
    w = closed_wire((0, 0), [
        ("L", (W, 0)), ("L", (W, t)), ("L", (b + rb, t)),
        ("A", (b + rb, t + rb), rb, 270, 180), ("L", (b, H - t - rb)),
        ("A", (b + rb, H - t - rb), rb, 180, 90), ("L", (W, H - t)),
        ("L", (W, H)), ("L", (0, H)), ("L", (0, H - t)), ("L", (a - rb, H - t)),
        ("A", (a - rb, H - t - rb), rb, 90, 0), ("L", (a, t + rb)),
        ("A", (a - rb, t + rb), rb, 0, -90), ("L", (0, t)),
    ])
    return cq.Face.makeFromWires(w)


def glyph_P(W):
    H, t, rb = CAP_H, SERIF_T, BRACKET_R
    s0 = P_STEM_AT * W             # stem left side
    s1 = s0 + STEM                 # stem right side
    uf = P_FOOT * W                # end of the foot serif
    vb = P_BOWL_AT * H             # bottom of the bowl
    rbow = (H - vb) / 2.0          # bowl radius
    ub = W - rbow                  # bowl arc centre
    outer = closed_wire((0, 0), [
        ("L", (uf, 0)), ("L", (uf, t)), ("L", (s1 + rb, t)),
        ("A", (s1 + rb, t + rb), rb, 270, 180), ("L", (s1, vb)), ("L", (ub, vb)),
        ("A", (ub, vb + rbow), rbow, -90, 90), ("L", (0, H)), ("L", (0, H - t)),
        ("L", (s0 - rb, H - t)), ("A", (s0 - rb, H - t - rb), rb, 90, 0),
        ("L", (s0, t + rb)), ("A", (s0 - rb, t + rb), rb, 0, -90), ("L", (0, t)),
    ])
    # counter of the bowl (left standing as a loose island, like the original)
    c1, cv0, cv1, rc = P_COUNTER * W, vb + 1.8, H - 2.4, 3.0
    counter = closed_wire((s1, cv0), [
        ("L", (c1 - rc, cv0)), ("A", (c1 - rc, cv0 + rc), rc, -90, 0),
        ("L", (c1, cv1 - rc)), ("A", (c1 - rc, cv1 - rc), rc, 0, 90),
        ("L", (s1, cv1)),
    ])
    return cq.Face.makeFromWires(outer, [counter])


def glyph_S(W):
    """S drawn as a stroke (two round bowls joined by a straight spine) in a
    horizontally compressed frame and then stretched, which thickens the
    upright parts of the curves; ball terminals at both ends"""
    k, w, r1, r2 = S_STRETCH, S_STROKE, S_R_UP, S_R_LOW
    a_top, a_bot = S_END_TOP, S_END_BOT
    v0, v1 = -0.2, CAP_H + 0.2                 # slight overshoot
    c1 = (S_LEFT / k + w / 2.0 + r1, v1 - w / 2.0 - r1)     # upper bowl
    c2 = (W / k - w / 2.0 - r2, v0 + w / 2.0 + r2)          # lower bowl
    # spine = inner common tangent, through the inner homothety centre
    hc = ((r2 * c1[0] + r1 * c2[0]) / (r1 + r2), (r2 * c1[1] + r1 * c2[1]) / (r1 + r2))
    gam = math.degrees(math.atan2(hc[1] - c1[1], hc[0] - c1[0]))
    alpha = math.degrees(math.acos(r1 / math.hypot(hc[0] - c1[0], hc[1] - c1[1])))
    ang1 = gam - alpha
    while ang1 < a_top:
        ang1 += 360.0
    ang2 = ang1 + 180.0
    while ang2 > a_bot + 360.0:
        ang2 -= 360.0
    while ang2 < a_bot:
        ang2 += 360.0
    p0, pm, p1 = arc3(c1, r1, a_top, ang1)
    q0, qm, q1 = arc3(c2, r2, ang2, a_bot)
    spine = (
        cq.Workplane("XY").moveTo(*p0).threePointArc(pm, p1)
        .lineTo(*q0).threePointArc(qm, q1).wire().val()
    )
    stretch = cq.Matrix([[k, 0.0, 0.0, 0.0], [0.0, 1.0, 0.0, 0.0], [0.0, 0.0, 1.0, 0.0]])
    stroke = cq.Face.makeFromWires(spine.offset2D(w / 2.0, "arc")[0].transformGeometry(stretch))
    balls = []
    for c, r, a in ((c1, r1, a_top), (c2, r2, a_bot)):
        ctr = cq.Vector(k * (c[0] + r * math.cos(math.radians(a))),
                        c[1] + r * math.sin(math.radians(a)), 0)
        balls.append(cq.Face.makeFromWires(
            cq.Wire.makeCircle(S_BALL_D / 2.0, ctr, cq.Vector(0, 0, 1))))
    return stroke.fuse(*balls).clean().Faces()[0]


def place(face, z0):
    """extrude a glyph face straight through the wall (along X) at height z0"""
    sol = cq.Solid.extrudeLinear(face, cq.Vector(0, 0, CUT_DEPTH))
    # local u -> +Z (reads upward), v -> +Y, extrusion -> -X (outward)
    sol = sol.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 1, 0), -90)
    return sol.translate(cq.Vector(X_CUT_IN, BASELINE_Y, z0))


cutters = [
    place(glyph_S(S_W), S_Z0),
    place(glyph_P(P_W), P_Z0),
    place(glyph_I(I_W), I_Z0),
]
dot_plane = cq.Plane(origin=(X_CUT_IN, BASELINE_Y, 0.0), xDir=(0, 0, 1), normal=(-1, 0, 0))
dots = (
    cq.Workplane(dot_plane)
    .pushPoints([(z, DOT_D / 2.0) for z in DOT_Z])
    .circle(DOT_D / 2.0)
    .extrude(CUT_DEPTH)
)
cutters += dots.solids().vals()

body = body.cut(cq.Workplane("XY").add(cq.Compound.makeCompound(cutters)))

result = body
